import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
# Two-piece enclosure: deep box (+X side) and flat lid/base tray (-X side)
GAP = 2.9            # gap between the two bodies along X

# ---- box (deep part)
BW = 58.6            # box width (X)
BL = 100.0           # box length (Y)
BH = 23.6            # box height incl. lip
WT = 2.0             # wall thickness
FT = 2.5             # floor thickness
LIP_H = 2.7          # lip height at the top
LIP_IN = 1.0         # lip inset from the outer face
R_V = 1.6            # vertical edge fillet
R_NOTCH = 1.5
R_BOT = 1.0
NOTCH_L = 12.3       # notch under the -Y end (length along Y)
NOTCH_H = 11.4       # notch height
PT = 1.6             # raised floor thickness over the notch
FRONT_CUT_X0 = 9.0   # lowered front wall starts here (from -X outer face)
FRONT_TOP = 17.6     # lowered front wall top
FRONT_STEP = 0.6     # outer step below the inner lip on the lowered wall
DIP_X0, DIP_X1, DIP_D = 29.4, 36.2, 1.0

SO_X = (6.0, 52.6)   # standoff X (from -X outer face)
SO_D = 4.4           # standoff dia
SO_HOLE = 1.6
TALL_H = 18.2        # tall standoff top (Z)
PLAT_SO_H = 18.2     # standoff on the raised floor (top Z)

VENT_N = 6
VENT_P = 5.5
VENT_Y0 = 11.0       # first slot centre from +Y outer face
VENT_W = 2.9           # wall groove width
VENT_FW = 2.4          # floor slot width
VENT_TOP = 13.0      # slot top height
VENT_IN = 9.0        # slot reach into floor from outer face
POCK_Y0, POCK_Y1 = 8.6, 40.5   # outside recess (from +Y face)
POCK_TOP = 13.8
POCK_D = 0.8
GROOVE_D = 1.6      # groove depth from outer face
LEDGE_W = 2.0
LEDGE_H = 1.6

# ---- base (flat tray)
TW = 58.2            # tray width
TL = 99.65           # tray length
TH = 5.5             # rim height
TF = 2.0             # tray floor thickness
T_LIP = 1.0          # outer lip thickness
T_LEDGE_W = 2.2      # total rim width
T_LEDGE_Z = 4.7
T_YOFF = -2.2        # tray -Y face relative to box -Y face

TSO_X = (5.7, 52.5)
TSO_Y_L = (5.3, 46.8, 89.0)     # -X side (from tray -Y face)
TSO_Y_R = (5.3, 46.8, 75.1)     # +X side
TSO_COLLAR_D = 6.0
TSO_COLLAR_H = 4.5
TSO_D = 4.4
TSO_TOP = 9.7
CB_D = 3.2           # counterbore under the tray standoffs
CB_DEP = 0.8

TV_N = 8
TV_P = 3.55
TV_Y0 = 10.2
TV_W = 1.7
TV_X = ((9.8, 23.9), (34.7, 48.5))

TAB_X0, TAB_X1 = 8.5, 57.1       # port frame at +Y end
TAB_OUT = 5.5
TAB_Z0, TAB_Z1 = 1.3, 10.8
TAB_T = 1.2
BUMP_X0, BUMP_X1, BUMP_H = 29.2, 36.2, 0.6
SLIT_W = 0.35
SLIT_D = 0.3         # engraved line depth (top and bottom)
SLITS = [            # (x0, y0, x1, y1) from tray -X / -Y faces
    (52.5, 46.8, 34.65, 35.4),
    (52.5, 46.8, 48.4, 31.5),
    (23.4, 31.5, 34.65, 35.05),
    (23.4, 31.5, 34.65, 30.8),
    (34.65, 10.2, 52.5, 5.3),
    (48.4, 10.2, 52.5, 5.3),
]
SLITS_BOTTOM = (0, 1, 5)   # lines also engraved on the underside
GROOVE_W = 1.6
GROOVE_DEP = 0.6
GROOVES = [(52.5, 46.8, 75.1), (5.7, 46.8, 89.0)]


def blk(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl(x, y, z0, z1, d):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(x, y).circle(d / 2.0).extrude(z1 - z0))


# ============================================================ BOX
bx0 = GAP / 2.0
bx1 = bx0 + BW
by0 = -BL / 2.0
by1 = BL / 2.0
zwall = BH - LIP_H

outer = (cq.Workplane("XY").workplane()
         .center(bx0 + BW / 2, 0).rect(BW, BL).extrude(zwall)
         .edges("|Z").fillet(R_V))
# notch under the -Y end
outer = outer.cut(blk(bx0 - 1, bx1 + 1, by0 - 1, by0 + NOTCH_L, -1, NOTCH_H))


def _notch_or_bottom(e):
    c = e.Center()
    if c.z < 0.01:
        return True
    return (c.y < by0 + NOTCH_L + 0.5 and c.z < NOTCH_H + 0.5)


_osol = outer.val()
_edges = [e for e in _osol.Edges() if _notch_or_bottom(e)]
outer = cq.Workplane("XY").newObject([_osol.fillet(R_NOTCH, _edges)])
lip = (cq.Workplane("XY").workplane(offset=zwall - 0.01)
       .center(bx0 + BW / 2, 0)
       .rect(BW - 2 * LIP_IN, BL - 2 * LIP_IN).extrude(LIP_H + 0.01)
       .edges("|Z").fillet(R_V - LIP_IN))
box = outer.union(lip)
# hollow: inner cavity follows the notch (raised floor over it)
cavity = blk(bx0 + WT, bx1 - WT, by0 + WT, by1 - WT, FT, BH + 1)
cavity = cavity.cut(blk(bx0, bx1, by0 - 1, by0 + NOTCH_L + WT, -1, NOTCH_H + PT))
box = box.cut(cavity)
# lowered front wall (outer step lower than inner lip)
box = box.cut(blk(bx0 + FRONT_CUT_X0, bx1 - WT, by0 - 1, by0 + WT + 0.01,
                  FRONT_TOP, BH + 1))
box = box.cut(blk(bx0 + FRONT_CUT_X0, bx1 - WT, by0 - 1, by0 + LIP_IN,
                  FRONT_TOP - FRONT_STEP, BH + 1))
box = box.cut(blk(bx0 + DIP_X0, bx0 + DIP_X1, by0 - 1, by0 + WT + 0.01,
                  FRONT_TOP - DIP_D, BH + 1))

# standoffs
so_list = [
    (SO_X[0], 5.2, TALL_H),
    (SO_X[1], 5.2, TALL_H),
    (SO_X[0], 46.8, TALL_H),
    (SO_X[1], 46.8, TALL_H),
    (SO_X[1], 75.1, TALL_H),
    (SO_X[0], 89.0, PLAT_SO_H),
]
for sx, sy, top in so_list:
    x = bx0 + sx
    y = by1 - sy
    zb = FT - 0.01 if sy < BL - NOTCH_L - WT else NOTCH_H + PT - 0.01
    box = box.union(cyl(x, y, zb, top, SO_D))
    box = box.cut(cyl(x, y, top - 5.0, top + 1, SO_HOLE))

# vents on both long walls: outside recess with blind grooves, slots
# through the floor edge, small ledge along the inner wall face
for side in (0, 1):
    sgn = -1 if side == 0 else 1
    xo = bx0 if side == 0 else bx1
    xi = xo - sgn * WT          # inner wall face
    yv0 = by1 - POCK_Y1
    yv1 = by1 - POCK_Y0
    # ledge on the inside
    lx0, lx1 = sorted((xi + 0.01 * sgn, xi - sgn * LEDGE_W))
    box = box.union(blk(lx0, lx1, yv0 + 1.0, yv1 - 1.0, FT - 0.01, FT + LEDGE_H))
    # outside recess
    px0, px1 = sorted((xo + sgn, xo - sgn * POCK_D))
    pk = blk(px0, px1, yv0, yv1, -1, POCK_TOP).edges("|X").edges(">Z").fillet(1.5)
    box = box.cut(pk)
    bq0, bq1 = sorted((xo + sgn, xo - sgn * (VENT_IN + 1.2)))
    box = box.cut(blk(bq0, bq1, yv0, yv1, -1, POCK_D))
    for i in range(VENT_N):
        yc = by1 - (VENT_Y0 + i * VENT_P)
        # blind vertical groove in the wall
        gx0, gx1 = sorted((xo + sgn, xo - sgn * GROOVE_D))
        g = (cq.Workplane("YZ").workplane(offset=gx0)
             .center(yc, (VENT_TOP - 1.0) / 2.0)
             .slot2D(VENT_TOP + 1.0, VENT_W, angle=90)
             .extrude(gx1 - gx0))
        box = box.cut(g)
        # through slot in the floor edge (wraps under the wall)
        fx0, fx1 = sorted((xo + sgn, xo - sgn * VENT_IN))
        fl = (cq.Workplane("XY").workplane(offset=-1)
              .center((fx0 + fx1) / 2.0, yc)
              .slot2D(fx1 - fx0, VENT_FW, angle=0)
              .extrude(FT + 1.0))
        box = box.cut(fl)

# ============================================================ BASE / TRAY
tx1 = -GAP / 2.0
tx0 = tx1 - TW
ty0 = by0 + T_YOFF
ty1 = ty0 + TL

tray = (cq.Workplane("XY").center(tx0 + TW / 2, ty0 + TL / 2)
        .rect(TW, TL).extrude(TH).edges("|Z").fillet(R_V))
tray = tray.faces("<Z").edges().fillet(0.8)
# ledge (inner step of the rim)
tray = tray.cut(blk(tx0 + T_LIP, tx1 - T_LIP, ty0 + T_LIP, ty1 - T_LIP,
                    T_LEDGE_Z, TH + 1))
# inner pocket down to the floor
tray = tray.cut(blk(tx0 + T_LEDGE_W, tx1 - T_LEDGE_W, ty0 + T_LEDGE_W,
                    ty1 - T_LEDGE_W, TF, TH + 1))

# port frame (rectangular sleeve) outside the +Y end, rim opened below it
frame = blk(tx0 + TAB_X0, tx0 + TAB_X1, ty1 - 0.01, ty1 + TAB_OUT,
            TAB_Z0, TAB_Z1)
frame = frame.union(blk(tx0 + BUMP_X0, tx0 + BUMP_X1, ty1 - 0.01,
                        ty1 + TAB_OUT, TAB_Z1 - 0.01, TAB_Z1 + BUMP_H))
tray = tray.union(frame)
tray = tray.cut(blk(tx0 + TAB_X0 + TAB_T, tx0 + TAB_X1 - TAB_T,
                    ty1 - 1, ty1 + TAB_OUT + 1,
                    TAB_Z0 + TAB_T, TAB_Z1 - TAB_T))
tray = tray.cut(blk(tx0 + TAB_X0 + TAB_T, tx0 + TAB_X1 - TAB_T,
                    ty1 - T_LEDGE_W - 0.01, ty1 + 0.01, TAB_Z0 + TAB_T,
                    TAB_Z1 - TAB_T))

# standoffs
for sx, ys in ((TSO_X[0], TSO_Y_L), (TSO_X[1], TSO_Y_R)):
    for sy in ys:
        x = tx0 + sx
        y = ty0 + sy
        tray = tray.union(cyl(x, y, TF - 0.01, TSO_COLLAR_H, TSO_COLLAR_D))
        tray = tray.union(cyl(x, y, TSO_COLLAR_H - 0.01, TSO_TOP, TSO_D))
        tray = tray.cut(cyl(x, y, -1, TSO_TOP + 1, SO_HOLE))
        tray = tray.cut(cyl(x, y, -1, CB_DEP, CB_D))

# vent slots
for (vx0, vx1) in TV_X:
    for i in range(TV_N):
        yc = ty0 + TV_Y0 + i * TV_P
        s = (cq.Workplane("XY").workplane(offset=-1)
             .center(tx0 + (vx0 + vx1) / 2.0, yc)
             .slot2D(vx1 - vx0, TV_W, angle=0).extrude(TF + 2))
        tray = tray.cut(s)

# thin engraved lines joining slot ends and standoffs (top and bottom)
for k, (xa, ya, xb, yb) in enumerate(SLITS):
    ax, ay = tx0 + xa, ty0 + ya
    bxx, byy = tx0 + xb, ty0 + yb
    ln = math.hypot(bxx - ax, byy - ay)
    ang = math.degrees(math.atan2(byy - ay, bxx - ax))
    zr = [(TF - SLIT_D, TSO_TOP + 1)]
    if k in SLITS_BOTTOM:
        zr.append((-1, SLIT_D))
    for z0, z1 in zr:
        sl = (cq.Workplane("XY").workplane(offset=z0)
              .center((ax + bxx) / 2, (ay + byy) / 2)
              .rect(ln, SLIT_W).extrude(z1 - z0)
              .rotate(((ax + bxx) / 2, (ay + byy) / 2, 0),
                      ((ax + bxx) / 2, (ay + byy) / 2, 1), ang))
        tray = tray.cut(sl)
# shallow grooves on the underside between standoffs
for (xa, ya, yb) in GROOVES:
    g = (cq.Workplane("XY").workplane(offset=-1)
         .center(tx0 + xa, ty0 + (ya + yb) / 2)
         .slot2D(yb - ya, GROOVE_W, angle=90).extrude(1 + GROOVE_DEP))
    tray = tray.cut(g)

result = box.union(tray)
